import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
# box (open-top enclosure), long axis along Y
W = 50.0          # outer width  (X)
L = 102.5         # outer length (Y)
H = 28.7          # outer height (Z)
T_WALL = 1.5      # side wall thickness
T_END_P = 1.7     # +Y end wall (the one with the window) is a little thicker
T_FLOOR = 1.6     # floor thickness
R_VERT = 2.5      # outer vertical corner radius
R_BOT = 2.0       # outer bottom edge radius
R_TOP = 0.7       # outer top (rim) edge radius

# rectangular opening in the floor (near +Y end)
RECT_W = 34.8
RECT_Y0, RECT_Y1 = 60.0, 79.5
RECT_R = 0.5
# round hole in the floor (near -Y end)
HOLE_D = 10.3
HOLE_Y = 28.8

# window in the +Y end wall
WIN_X0, WIN_X1 = 15.8, 36.9
WIN_Z0, WIN_Z1 = 8.8, 19.5

# notch at the bottom of the +X wall next to the +Y end
NOTCH_DEPTH = 3.3         # from the outer +X face inward
NOTCH_Y0 = L - 10.5
NOTCH_Y1 = L + 1.0
NOTCH_Z1 = 12.6

# lid (lying beside the box, inside face up)
GAP = 24.2         # gap between box and lid in X
LID_DY = 1.85      # lid offset along Y
LID_T = 1.3        # base plate thickness
LID_R = 3.6        # base plate corner radius
LIP_OFF = 1.6      # inset of the plug from the plate edge
LIP_T = 1.3        # plug thickness
LIP_R = 2.4
LID_EDGE_R = 0.9   # rounded top edge of the base plate
LIP_EDGE_R = 0.2   # small break on the plug top edge
REC_D = 0.3        # shallow label recess in the plug
REC_XM, REC_XP = 3.4, 2.8    # recess offsets from lid outer edges
REC_YM, REC_YP = 5.2, 2.8
REC_R = 0.5        # small corner radius of the recess

# ---------------- box ----------------
box = (
    cq.Workplane("XY")
    .box(W, L, H, centered=(False, False, False))
    .edges("|Z").fillet(R_VERT)
    .faces("<Z").edges().fillet(R_BOT)
    .faces(">Z").edges().fillet(R_TOP)
)

cavity = (
    cq.Workplane("XY", origin=(0, 0, T_FLOOR))
    .center(W / 2, (T_WALL + (L - T_END_P)) / 2)
    .rect(W - 2 * T_WALL, L - T_WALL - T_END_P)
    .extrude(H)
)
box = box.cut(cavity)

# floor openings
rect_hole = (
    cq.Workplane("XY", origin=(0, 0, -1))
    .center(W / 2, (RECT_Y0 + RECT_Y1) / 2)
    .sketch()
    .rect(RECT_W, RECT_Y1 - RECT_Y0)
    .vertices()
    .fillet(RECT_R)
    .finalize()
    .extrude(T_FLOOR + 2)
)
round_hole = (
    cq.Workplane("XY", origin=(0, 0, -1))
    .center(W / 2, HOLE_Y)
    .circle(HOLE_D / 2)
    .extrude(T_FLOOR + 2)
)
box = box.cut(rect_hole).cut(round_hole)

# window in +Y end wall
window = (
    cq.Workplane("XY")
    .box(WIN_X1 - WIN_X0, 4 * T_END_P, WIN_Z1 - WIN_Z0, centered=False)
    .translate((WIN_X0, L - 2 * T_END_P, WIN_Z0))
)
box = box.cut(window)

# notch through the +X wall and floor near the +Y end
notch = (
    cq.Workplane("XY")
    .box(NOTCH_DEPTH + 2, NOTCH_Y1 - NOTCH_Y0, NOTCH_Z1 + 1, centered=False)
    .translate((W - NOTCH_DEPTH, NOTCH_Y0, -1))
)
box = box.cut(notch)

# ---------------- lid ----------------
lx0 = W + GAP
ly0 = LID_DY
plate = (
    cq.Workplane("XY")
    .box(W, L, LID_T, centered=False)
    .edges("|Z").fillet(LID_R)
    .faces(">Z").edges().fillet(LID_EDGE_R)
)
plug = (
    cq.Workplane("XY")
    .box(W - 2 * LIP_OFF, L - 2 * LIP_OFF, LIP_T, centered=False)
    .edges("|Z").fillet(LIP_R)
    .faces(">Z").edges().fillet(LIP_EDGE_R)
    .translate((LIP_OFF, LIP_OFF, LID_T))
)
lid = plate.union(plug)
recess = (
    cq.Workplane("XY", origin=(0, 0, LID_T + LIP_T - REC_D))
    .center((REC_XM + W - REC_XP) / 2, (REC_YM + L - REC_YP) / 2)
    .sketch()
    .rect(W - REC_XM - REC_XP, L - REC_YM - REC_YP)
    .vertices()
    .fillet(REC_R)
    .finalize()
    .extrude(2)
)
lid = lid.cut(recess).translate((lx0, ly0, 0))

result = box.union(lid)
